import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 300.0          # plate width  (X)
H = 240.0          # plate height (Z)
T = 6.0            # plate thickness (Y), front face at Y=0, back at Y=T

# mounting slots (obround, horizontal)
SLOT_L = 16.0
SLOT_W = 8.4
SLOT_X = (-91.6, 117.6)
SLOT_Z = (83.5, -85.3)

# stand-off pins (tubes on the back face)
PIN_X = (-11.2, 134.9)
PIN_Z = (105.7, 5.0)
PIN_D = 19.0
PIN_L = 49.3
PIN_BORE = 7.0
PIN_CHAMFER = 0.4
PIN_ID = 17.0         # tube inner diameter
PIN_SEAM_DEG = 225.0   # where the cylinder seam sits (hidden side)

# small lugs on the back face at the top and bottom edges (pairs)
TAB_PAIR_X = (-45.5, 100.0)   # pair centres
TAB_OFF = 6.8                 # tab centre offset from pair centre
TAB_W = 4.0                   # along X
TAB_D = 7.2                   # protrusion along +Y
TAB_H = 7.0                   # along Z (from the plate edge inwards)
TAB_RX = 4.2                  # outer-side base fillet (XY)
TAB_RZ = 4.5                  # inner-side base fillet (YZ)
TAB_RT = 0.8                  # rounded top corners (XY)
TAB_RC = 1.2                  # rounded outer corner (YZ)

# embossed marking on the back face
TEXT = "ASA"
TEXT_SIZE = 12.5
TEXT_H = 2.6
TEXT_X = -28.5
TEXT_Z = -43.5

VIEW = {"azimuth": 45, "elevation": 26}

EPS = 0.5

# ---------------- plate ----------------
plate = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(-T)          # XZ normal is -Y, so negative extrude goes to +Y
)

# slots through the plate
slot_pts = [(x, z) for x in SLOT_X for z in SLOT_Z]
slots = (
    cq.Workplane("XZ", origin=(0, -1, 0))
    .pushPoints(slot_pts)
    .slot2D(SLOT_L, SLOT_W, 0)
    .extrude(-(T + 2))
)
plate = plate.cut(slots)

# ---------------- pins ----------------
a = math.radians(PIN_SEAM_DEG)
pins = None
for px in PIN_X:
    for pz in PIN_Z:
        pl = cq.Plane(
            origin=(px, T - EPS, pz),
            xDir=(math.cos(a), 0, math.sin(a)),
            normal=(0, 1, 0),
        )
        p = cq.Workplane(pl).circle(PIN_D / 2).extrude(PIN_L + EPS)
        p = p.faces(">Y").edges().chamfer(PIN_CHAMFER)
        pins = p if pins is None else pins.union(p)
body = plate.union(pins)

# through bore (plate + pin)
pin_pts = [(x, z) for x in PIN_X for z in PIN_Z]
bores = (
    cq.Workplane("XZ", origin=(0, -1, 0))
    .pushPoints(pin_pts)
    .circle(PIN_BORE / 2)
    .extrude(-(T + PIN_L + 2))
)
body = body.cut(bores)

# tube bore from the pin end down to the plate back face
tubes = (
    cq.Workplane("XZ", origin=(0, T, 0))
    .pushPoints(pin_pts)
    .circle(PIN_ID / 2)
    .extrude(-(PIN_L + 1))
)
body = body.cut(tubes)


# ---------------- tabs ----------------
def make_tab(xc, side, edge):
    """xc: tab centre X, side: +1/-1 direction of the outer X fillet,
    edge: +1 top edge, -1 bottom edge."""
    hw = TAB_W / 2
    # XY profile (local u = X offset * side, v = Y from back face)
    m = 1 - math.sqrt(0.5)
    rt = TAB_RT
    w = cq.Workplane("XY").moveTo(-hw, -EPS).lineTo(-hw, TAB_D - rt)
    w = w.threePointArc((-hw + rt * m, TAB_D - rt * m), (-hw + rt, TAB_D))
    w = w.lineTo(hw - rt, TAB_D)
    w = w.threePointArc((hw - rt * m, TAB_D - rt * m), (hw, TAB_D - rt))
    w = w.lineTo(hw, TAB_RX)
    w = w.threePointArc((hw + TAB_RX * m, TAB_RX * m), (hw + TAB_RX, 0))
    w = w.lineTo(hw + TAB_RX, -EPS).close()
    zlen = TAB_H + TAB_RZ + 1
    prism_xy = w.extrude(zlen)
    if side < 0:
        prism_xy = prism_xy.mirror("YZ")
    prism_xy = prism_xy.translate((xc, T, 0))
    if edge > 0:
        prism_xy = prism_xy.translate((0, 0, H / 2 - zlen + 0.5))
    else:
        prism_xy = prism_xy.translate((0, 0, -H / 2 - 0.5))

    # YZ profile (local u = Y from back face, v = distance from plate edge)
    w2 = (
        cq.Workplane("YZ")
        .moveTo(-EPS, 0)
        .lineTo(TAB_D, 0)
        .lineTo(TAB_D, TAB_H - TAB_RC)
        .threePointArc(
            (TAB_D - TAB_RC * m, TAB_H - TAB_RC * m), (TAB_D - TAB_RC, TAB_H)
        )
        .lineTo(TAB_RZ, TAB_H)
        .threePointArc((TAB_RZ * m, TAB_H + TAB_RZ * m), (0, TAB_H + TAB_RZ))
        .lineTo(-EPS, TAB_H + TAB_RZ)
        .close()
    )
    xlen = TAB_W + 2 * TAB_RX + 2
    prism_yz = w2.extrude(xlen).translate((xc - xlen / 2, T, 0))
    if edge > 0:
        # v measured downward from the top edge
        prism_yz = prism_yz.mirror("XY").translate((0, 0, H / 2))
    else:
        prism_yz = prism_yz.translate((0, 0, -H / 2))
    return prism_xy.intersect(prism_yz)


tabs = None
for pc in TAB_PAIR_X:
    for s in (-1, 1):
        for e in (1, -1):
            t = make_tab(pc + s * TAB_OFF, s, e)
            tabs = t if tabs is None else tabs.union(t)
body = body.union(tabs)

# ---------------- embossed text on the back ----------------
try:
    tpl = cq.Plane(origin=(TEXT_X, T - 0.3, TEXT_Z), xDir=(0, 0, -1), normal=(0, 1, 0))
    txt = cq.Workplane(tpl).text(
        TEXT, TEXT_SIZE, TEXT_H + 0.3, halign="center", valign="center"
    )
    body = body.union(txt)
except Exception:
    pass

result = body
